import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Robot arm base: octagonal motor housing (hollow from the back), turntable
# disc + hub, clevis blocks, and a double-parallelogram planar linkage arm.
# Built in a local frame (x across the housing, arm reaching toward -y,
# z up), then the whole assembly is tilted about the Y axis.
# ---------------------------------------------------------------------------

TILT = 16.5            # deg, rotation of the whole assembly about Y

# --- octagonal housing ------------------------------------------------------
W = 149.0              # flat-to-flat width of the octagon
CH = 19.6              # corner chamfer leg
T = 38.0               # housing thickness (Y)
WALL = 3.0             # shell wall thickness
FRONT_WALL = 4.0       # front wall thickness
CYL_D = 110.0          # inner motor cylinder diameter
CYL_RECESS = 8.0       # recess of cylinder face below rim
RING_D = 46.0          # centre ring diameter
RING_DEPTH = 2.0

# --- turntable ---------------------------------------------------------------
DISC_D = 104.0
DISC_T = 4.5
HUB_D = 66.0
HUB_T = 7.0
HUB_CHAMFER = 1.5
HUB_HOLE_D = 14.0
HUB_HOLE_X = 17.4
HUB_HOLE_Z = 11.5
HUB_HOLE_DEPTH = 3.0

# --- clevis blocks -----------------------------------------------------------
BLK_W = 77.0
BLK_H = 31.5
BLK_D = 33.5
BLK_GAP = 24.0
SHOULDER_HOLE = 18.0
SHOULDER_DEPTH = 20.0

# --- linkage key points (x, y) in the local frame ---------------------------
S = (0.0, -28.5)        # shoulder pivot (axis of the block holes)
P1 = (30.0, -63.0)      # crank pin
C = (4.1, -188.5)       # elbow outer pin
D = (-29.8, -150.0)     # elbow pin of the wide upper bar
E = (-43.5, -183.0)     # elbow pin of the outer forearm bar
A = (-119.5, 33.9)      # wrist pin (inner forearm bar)
B = (-135.5, 1.2)       # wrist pin (outer forearm bar)
WCORNER = (-153.4, 40.5)  # outer corner of the wrist bracket
WLEFT_BOT = (-142.1, -1.5)  # lower end of the bracket's outer edge
NOTCH_X = -126.7        # inner notch edge of the wrist bracket
F1TOP = (-129.7, 1.0)   # top end of outer forearm bar
F2END = (-37.4, -168.0)  # square lower end of inner forearm bar
U2_ARM = (24.0, -37.0)  # short lever arm of the wide upper bar
ELB_END = (6.0, -186.0)  # centre of the rounded end of the elbow block
ELB_R = 7.5
BR1 = ((-24.5, -150.5), (-0.3, -159.5))   # elbow cross brace (upper)
BR2 = ((-25.7, -176.5), (-3.3, -167.2))   # elbow cross brace (lower)
ELB_PTS = [(-33.0, -186.0), (6.0, -193.5), (6.0, -178.5), (-25.0, -172.0),
           (-40.0, -172.0), (-40.0, -180.0)]
L3_TOP = (22.0, -28.2)  # lower tie bar pivot on the lower block
L3_END = (-3.0, -175.0)  # lower tie bar elbow end

PIN_D = 5.5

# levels (local z) of the linkage layers
Z_U1 = (5.5, 10.5)      # outer upper-arm bar
Z_CR = (6.5, 12.0)      # crank plate (bears on the upper block)
Z_U2 = (0.0, 6.0)       # wide upper-arm bar
Z_ELB = (-6.5, 5.5)     # thick elbow block
Z_F2 = (-4.0, 3.5)      # inner forearm bar
Z_F1 = (-15.0, -4.0)    # outer forearm bar body
Z_F1TAB = (-15.0, -9.0)  # thin end tab of the outer forearm bar at E
Z_WT = (5.0, 10.0)      # wrist top plate
Z_WB = (-18.5, -13.5)   # wrist bottom plate
Z_L3 = (-12.0, -9.5)    # lower tie bar
Z_BR = (-4.0, -1.0)     # elbow cross braces


def octagon_pts(w, c):
    h = w / 2.0
    return [(-h + c, -h), (h - c, -h), (h, -h + c), (h, h - c),
            (h - c, h), (-h + c, h), (-h, h - c), (-h, -h + c)]


def zcyl(p, d, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).center(*p)
            .circle(d / 2.0).extrude(z1 - z0))


def bar(p, q, width, zr, holes=(), hole_d=PIN_D):
    z0, z1 = zr
    dx, dy = q[0] - p[0], q[1] - p[1]
    L = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    mid = ((p[0] + q[0]) / 2.0, (p[1] + q[1]) / 2.0)
    b = (cq.Workplane("XY").workplane(offset=z0).center(*mid)
         .slot2D(L + width, width, ang).extrude(z1 - z0))
    for pt in holes:
        b = b.cut(zcyl(pt, hole_d, z0 - 1, z1 + 1))
    return b


def strip(p, q, w0, w1, zr, round_p=True, round_q=False):
    """Straight strip from p to q, width w0 at p and w1 at q."""
    z0, z1 = zr
    dx, dy = q[0] - p[0], q[1] - p[1]
    L = math.hypot(dx, dy)
    nx, ny = -dy / L, dx / L
    pts = [(p[0] + nx * w0 / 2, p[1] + ny * w0 / 2),
           (q[0] + nx * w1 / 2, q[1] + ny * w1 / 2),
           (q[0] - nx * w1 / 2, q[1] - ny * w1 / 2),
           (p[0] - nx * w0 / 2, p[1] - ny * w0 / 2)]
    s = (cq.Workplane("XY").workplane(offset=z0).polyline(pts).close()
         .extrude(z1 - z0))
    if round_p:
        s = s.union(zcyl(p, w0, z0, z1))
    if round_q:
        s = s.union(zcyl(q, w1, z0, z1))
    return s


def poly_plate(pts, zr):
    z0, z1 = zr
    return (cq.Workplane("XY").workplane(offset=z0).polyline(pts).close()
            .extrude(z1 - z0))


def along(p, q, t, off=0.0):
    dx, dy = q[0] - p[0], q[1] - p[1]
    L = math.hypot(dx, dy)
    nx, ny = -dy / L, dx / L
    return (p[0] + dx * t + nx * off, p[1] + dy * t + ny * off)


# ---------------------------------------------------------------------------
# Housing (octagon in XZ plane, y = 0 .. T), hollow from the back
# ---------------------------------------------------------------------------
housing = (cq.Workplane("XZ").polyline(octagon_pts(W, CH)).close()
           .extrude(-T))
inner = (cq.Workplane("XZ").workplane(offset=-FRONT_WALL)
         .polyline(octagon_pts(W - 2 * WALL, CH - WALL * 0.41)).close()
         .extrude(-(T - FRONT_WALL) - 1))
housing = housing.cut(inner)
motor = (cq.Workplane("XZ").workplane(offset=-FRONT_WALL)
         .circle(CYL_D / 2.0).extrude(-(T - FRONT_WALL - CYL_RECESS)))
housing = housing.union(motor)
ring = (cq.Workplane("XZ").workplane(offset=-(T - CYL_RECESS - RING_DEPTH))
        .circle(RING_D / 2.0).circle(RING_D / 2.0 - 2.0)
        .extrude(-RING_DEPTH - 1))
housing = housing.cut(ring)

# turntable disc and hub (in front, -Y)
disc = cq.Workplane("XZ").circle(DISC_D / 2.0).extrude(DISC_T)
hub = (cq.Workplane("XZ").workplane(offset=DISC_T)
       .circle(HUB_D / 2.0).extrude(HUB_T)
       .faces("<Y").edges().chamfer(HUB_CHAMFER))
base = housing.union(disc).union(hub)

# clevis blocks
y_blk0 = -(DISC_T + HUB_T)
y_blk1 = y_blk0 - BLK_D
ztop = BLK_GAP / 2.0 + BLK_H
for sgn in (1, -1):
    zc = sgn * (BLK_GAP / 2.0 + BLK_H / 2.0)
    blk = (cq.Workplane("XY").box(BLK_W, BLK_D, BLK_H)
           .translate((0, (y_blk0 + y_blk1) / 2.0, zc)))
    base = base.union(blk)
# shoulder holes (blind from outer faces)
base = base.cut(zcyl(S, SHOULDER_HOLE, ztop - SHOULDER_DEPTH, ztop + 1))
base = base.cut(zcyl(S, SHOULDER_HOLE, -ztop - 1, -ztop + SHOULDER_DEPTH))
# small hole at corner of upper block
base = base.cut(zcyl((-33.0, -42.0), 3.0, ztop - 6, ztop + 1))
# shallow bolt holes in the hub face (seen through the clevis gap)
for hx in (-HUB_HOLE_X, HUB_HOLE_X):
    for hz in (-HUB_HOLE_Z, HUB_HOLE_Z):
        base = base.cut(cq.Workplane("XZ").workplane(offset=DISC_T + HUB_T)
                        .center(hx, hz).circle(HUB_HOLE_D / 2.0)
                        .extrude(-HUB_HOLE_DEPTH))

# ---------------------------------------------------------------------------
# Linkage
# ---------------------------------------------------------------------------
parts = []
# slim shoulder pin spanning the clevis gap
parts.append(zcyl(S, 8.0, Z_U2[0], BLK_GAP / 2.0))
# crank plate S -> P1 and outer upper-arm bar P1 -> C
parts.append(strip(P1, S, 14.0, 24.0, Z_CR, round_p=True, round_q=True))
parts.append(bar(P1, C, 15.5, Z_U1, holes=[C]))
parts.append(zcyl(P1, 11.0, Z_CR[1], Z_CR[1] + 2.0))
parts.append(zcyl(P1, PIN_D, Z_CR[1] + 2.0, 23.0))
# wide upper-arm bar S -> D with stepped narrowing near the elbow
step0 = along(S, D, 0.70)
step1 = along(S, D, 0.80)
parts.append(strip(S, step0, 25.0, 24.0, Z_U2, round_p=True))
parts.append(bar(S, U2_ARM, 12.0, Z_U2))
parts.append(strip(step0, step1, 24.0, 13.0, Z_U2, round_p=False))
parts.append(strip(step1, D, 13.0, 13.0, Z_U2, round_p=False, round_q=True))
# thick elbow block with a rounded outer end
elbow = poly_plate(ELB_PTS, Z_ELB).union(zcyl(ELB_END, ELB_R * 2.0, *Z_ELB))
elbow = elbow.cut(zcyl(C, PIN_D + 1.0, Z_ELB[0] - 1, Z_ELB[1] + 1))
parts.append(elbow)
parts.append(zcyl(D, 8.0, Z_U2[1], Z_U2[1] + 3.0))
# cross braces of the elbow
parts.append(bar(BR1[0], BR1[1], 5.0, Z_BR))
parts.append(bar(BR2[0], BR2[1], 5.0, Z_BR))
for br in (BR1, BR2):
    parts.append(zcyl(br[1], 4.5, Z_L3[1], Z_BR[0]))
parts.append(zcyl(BR1[0], 4.5, Z_BR[1], Z_U2[0]))
# inner forearm bar A -> F2END (square end) with two small holes
f2 = strip(A, F2END, 16.0, 16.0, Z_F2, round_p=True, round_q=False)
for t in (0.86, 0.91):
    f2 = f2.cut(zcyl(along(A, F2END, t), 2.5, Z_F2[0] - 1, Z_F2[1] + 1))
parts.append(f2)
# outer forearm bar F1TOP -> E (widened under the inner bar)
F1_BODY_END = along(F1TOP, E, 0.88)
parts.append(strip(F1TOP, F1_BODY_END, 13.0, 13.0, Z_F1, round_p=True))
parts.append(strip(along(F1TOP, E, 0.08, 6.0), along(F1TOP, E, 0.88, 6.0),
                   12.0, 12.0, Z_F1, round_p=False))
parts.append(bar(along(F1TOP, E, 0.85), E, 13.0, Z_F1TAB, holes=[E]))
# wrist bracket (top and bottom L-plates, outer wall) and posts
wr = [WCORNER, (A[0] + 4.1, WCORNER[1]), (A[0] + 6.0, A[1]),
      (A[0] + 5.5, A[1] - 4.4), (NOTCH_X, A[1] - 7.1), (NOTCH_X, B[1]),
      (B[0], B[1] - 6.0), (WLEFT_BOT[0], WLEFT_BOT[1])]
for zr in (Z_WT, Z_WB):
    wp = poly_plate(wr, zr).union(zcyl(A, 12.0, *zr)).union(zcyl(B, 12.0, *zr))
    for pt in (A, B):
        wp = wp.cut(zcyl(pt, PIN_D, zr[0] - 1, zr[1] + 1))
    parts.append(wp)
parts.append(zcyl(A, 9.0, Z_WB[1], Z_WT[0]))
parts.append(zcyl(B, 8.0, Z_WB[1], Z_WT[0]))
# outer side wall of the wrist bracket (makes it a C-channel)
WALL_T = 4.0
parts.append(strip(along(WLEFT_BOT, WCORNER, 0.35, -WALL_T / 2.0),
                   along(WLEFT_BOT, WCORNER, 1.0, -WALL_T / 2.0),
                   WALL_T, WALL_T, (Z_WB[0], Z_WT[1]), round_p=False))
# lower tie bar from the clevis gap to the elbow
parts.append(bar(L3_TOP, L3_END, 7.0, Z_L3, holes=[L3_TOP, L3_END],
                 hole_d=3.5))

arm = parts[0]
for p in parts[1:]:
    arm = arm.union(p)

result = base.union(arm)
result = result.rotate((0, 0, 0), (0, 1, 0), -TILT)

VIEW = {"azimuth": 45, "elevation": 26}
